import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_SPOKES = 7            # spokes / handles / heptagon sides
RIM_R_OUT = 100.0       # rim outer radius
RIM_R_IN = 79.5         # rim inner radius
RIM_T = 20.5            # rim thickness (axial)
HUB_R = 30.5            # hub radius
HUB_T = 25.0            # hub thickness (axial)
BORE_R = 14.0           # heptagonal bore circumradius
SPOKE_D_HUB = 22.5      # spoke diameter at hub end
SPOKE_D_RIM = 17.8      # spoke diameter at rim end
SPOKE_FILLET = 5.0      # spoke-to-hub blend radius
WEB_R = 8.5             # blend radius between neighbouring spokes

HANDLE_LEN = 36.8       # handle length beyond rim outer surface
COLLAR_R = 8.1          # collar radius
COLLAR_T = 2.5          # collar thickness
NECK_R = 5.4            # smallest neck radius
BULB_R = 8.0            # bulb radius

SPOKE0_DEG = 7.0        # angular position of first spoke
TILT_DEG = -6.0         # tilt of the wheel plane about Y

# ---------------- rim ----------------
rim = (cq.Workplane("XY").workplane(offset=-RIM_T / 2.0)
       .circle(RIM_R_OUT).circle(RIM_R_IN)
       .extrude(RIM_T)
       .rotate((0, 0, 0), (0, 0, 1), SPOKE0_DEG))

# ---------------- hub ----------------
hub = (cq.Workplane("XY").workplane(offset=-HUB_T / 2.0)
       .circle(HUB_R).extrude(HUB_T)
       .rotate((0, 0, 0), (0, 0, 1), SPOKE0_DEG))

# ---------------- spokes (tapered round bars) ----------------
# Each spoke is a cone buried a little in the hub and in the rim.
spoke_r0 = HUB_R - 6.0
spoke_r1 = RIM_R_IN + 3.0
taper = (SPOKE_D_HUB - SPOKE_D_RIM) / 2.0 / (RIM_R_IN - HUB_R)   # dR/dr
rho_c = SPOKE_D_HUB / 2.0 + taper * HUB_R    # spoke radius extrapolated to axis
HALF = math.pi / N_SPOKES                    # half angle between spokes


def spoke_dir(k):
    a = math.radians(SPOKE0_DEG) + 2.0 * HALF * k
    return cq.Vector(math.cos(a), math.sin(a), 0)


def make_spoke(k):
    d = spoke_dir(k)
    r_start = rho_c - taper * spoke_r0
    r_end = rho_c - taper * spoke_r1
    return cq.Solid.makeCone(r_start, r_end, spoke_r1 - spoke_r0, d * spoke_r0, d)


def make_web(k):
    """Blend filling the crotch between spoke k and spoke k+1 next to the hub.

    Rolling-ball blend of radius WEB_R between two spokes: the region lying
    within (spoke radius + WEB_R) of both spoke axes, minus the tube swept by
    the ball along its spine (an ellipse in the bisector plane)."""
    th_m = math.radians(SPOKE0_DEG) + 2.0 * HALF * k + HALF
    m = cq.Vector(math.cos(th_m), math.sin(th_m), 0)
    nrm = cq.Vector(-math.sin(th_m), math.cos(th_m), 0)
    big = rho_c + WEB_R
    kp = taper * math.cos(HALF)
    alpha = math.sin(HALF) ** 2 - kp ** 2
    s0 = -big * kp / alpha
    a_z = big * math.sqrt(1.0 + kp ** 2 / alpha)
    a_s = a_z / math.sqrt(alpha)
    length = 60.0
    ea = cq.Solid.makeCone(big, big - taper * length, length,
                           cq.Vector(0, 0, 0), spoke_dir(k))
    eb = cq.Solid.makeCone(big, big - taper * length, length,
                           cq.Vector(0, 0, 0), spoke_dir(k + 1))
    h = HUB_T / 2.0 - 0.25
    ring = (cq.Workplane("XY").workplane(offset=-h)
            .circle(HUB_R + 12.0).circle(HUB_R - 1.0).extrude(2.0 * h)).val()
    lens = ea.intersect(eb).intersect(ring)
    spine = cq.Wire.assembleEdges([cq.Edge.makeEllipse(a_s, a_z, m * s0, nrm, m)])
    ball = cq.Wire.makeCircle(WEB_R, m * (s0 + a_s), cq.Vector(0, 0, 1))
    tube = cq.Solid.sweep(ball, [], spine, True, False)
    return lens.cut(tube)


hub_box = cq.selectors.BoxSelector((-HUB_R - 8, -HUB_R - 8, -HUB_T),
                                   (HUB_R + 8, HUB_R + 8, HUB_T))
# one sector = hub + spoke blended into it, plus the web to the next spoke;
# the sector is patterned around the axis and the copies fused (fuzzy, since
# the blends of neighbouring spokes overlap).
sector = hub.union(cq.Workplane("XY").add(make_spoke(0)))
try:
    sector = sector.edges(hub_box).edges("%BSPLINE").fillet(SPOKE_FILLET)
except Exception as exc:
    print('spoke fillet skipped:', exc)
sector = sector.val()


def about_axis(shape, k):
    return shape.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1),
                        k * 360.0 / N_SPOKES)


star = sector
for k in range(1, N_SPOKES):
    star = star.fuse(about_axis(sector, k), tol=1e-3)
try:
    web = make_web(0)
    webbed = star
    for k in range(N_SPOKES):
        webbed = webbed.fuse(about_axis(web, k), tol=1e-3)
    webbed = webbed.clean()
    if webbed.isValid() and len(webbed.Solids()) == 1:
        star = webbed
except Exception as exc:
    print('web blends skipped:', exc)
hub_spokes = cq.Workplane("XY").add(star.clean())

# ---------------- handles (revolved profile) ----------------
def make_handle():
    """Belaying-pin style handle, axis along +X, base at x=0 (rim surface)."""
    c = HANDLE_LEN - BULB_R            # centre of the rounded bulb end

    def on_bulb(deg):
        a = math.radians(deg)
        return cq.Vector(c + BULB_R * math.cos(a), BULB_R * math.sin(a), 0)

    def bulb_tan(deg):
        a = math.radians(deg)
        return cq.Vector(math.sin(a), -math.cos(a), 0)

    p_start = cq.Vector(COLLAR_T, COLLAR_R - 1.1, 0)
    pts = [p_start,
           cq.Vector(COLLAR_T + 6.5, NECK_R, 0),          # waist of the neck
           cq.Vector(COLLAR_T + 14.0, NECK_R + 1.0, 0),
           on_bulb(90), on_bulb(45), on_bulb(0)]
    tans = [cq.Vector(1, -0.9, 0), cq.Vector(1, 0, 0), cq.Vector(1, 0.2, 0),
            bulb_tan(90), bulb_tan(45), bulb_tan(0)]
    body = cq.Edge.makeSpline(pts, tangents=tans, scale=True)
    a0 = cq.Vector(-4.0, 0, 0)
    a1 = cq.Vector(-4.0, COLLAR_R, 0)
    a2 = cq.Vector(COLLAR_T, COLLAR_R, 0)
    tip = cq.Vector(HANDLE_LEN, 0, 0)
    wire = cq.Wire.assembleEdges([
        cq.Edge.makeLine(a0, a1),
        cq.Edge.makeLine(a1, a2),
        cq.Edge.makeLine(a2, p_start),
        body,
        cq.Edge.makeLine(tip, a0)])
    face = cq.Face.makeFromWires(wire)
    return cq.Solid.revolve(face, 360.0, cq.Vector(0, 0, 0), cq.Vector(1, 0, 0))


# turn the revolve seam of the handle to its underside
handle_proto = make_handle().rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -90)
wheel = rim.union(hub_spokes)
for k in range(N_SPOKES):
    ang = SPOKE0_DEG + k * 360.0 / N_SPOKES
    h = (handle_proto.translate(cq.Vector(RIM_R_OUT - 0.5, 0, 0))
         .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ang))
    wheel = wheel.union(cq.Workplane("XY").add(h))

# ---------------- heptagonal bore ----------------
bore = (cq.Workplane("XY")
        .polygon(N_SPOKES, 2 * BORE_R)
        .extrude(HUB_T, both=True)
        .rotate((0, 0, 0), (0, 0, 1), SPOKE0_DEG + 180.0 / N_SPOKES))
wheel = wheel.cut(bore)

# ---------------- orientation ----------------
result = wheel.rotate((0, 0, 0), (0, 1, 0), TILT_DEG)

VIEW = {"azimuth": 45, "elevation": 26}
